import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Split (V-shaped, "Alice"-style) keyboard bottom tray.
# Thin-walled tray: flat floor, perimeter wall following a stepped outline,
# screw posts in the corners, a cable slot at the centre of the back "V",
# and a concave scooped front between the two wings.
# Layout is drafted in a unit U and scaled to millimetres by S.
# ---------------------------------------------------------------------------
S = 1.6                 # mm per drafting unit

# --- overall / shell --------------------------------------------------------
H = 8.7 * S             # total height of tray
FLOOR = 1.7 * S         # floor thickness
WALL = 2.0 * S          # wall thickness

# --- wing (left half, mirrored for the right) --------------------------------
WING_ANG = 15.0                     # wing rotation (deg, clockwise for left wing)
WING_ORG = (-104.18, 57.06)         # back-left outer corner of left wing (units)
WING_DEPTH = 57.6                   # front-to-back depth of wing
WING_FRONT_LEN = 50.0               # length of wing front edge before the step
FRONT_STEP = 11.7                   # step out at the front of the wing
STEP1_U, STEP1_V = 18.7, 9.0        # first raised section of back edge
STEP2_U, STEP2_V = 36.6, 12.5       # second raised section of back edge
STEP3_U = 58.8                      # end of raised section
V_EDGE_V = 7.4                      # offset of the centre V edge

# --- centre front (scoop) -------------------------------------------------------
FRONT_Y = -60.6                     # y of flat front edge
FRONT_HALF = 15.65                  # half length of flat front edge
SCOOP_START_ANG = 15.0              # scoop leaves the wing step along the wing
SCOOP_END_ANG = 52.0                # heading where scoop meets the front flat
SCOOP_SAG = 6.5                     # depth of scoop at mid-chord (units)

# --- corner treatment ---------------------------------------------------------
R_BOSS_CORNER = 4.0                 # outer corner radius at screw posts
R_STEP_CORNER = 4.5                 # outer corner where the scoop leaves the wing step
R_CONVEX = 4.0                      # other outside corners
R_STEP_DOWN = 3.0                   # outside corner where the back edge steps down to the V
R_SMALL_STEP = 2.6                  # outside corner of the small back step
R_CONCAVE = 2.0                     # inside corners
R_CONCAVE_B = 1.5                   # inside corner at the foot of the V step
R_CONCAVE_E = 0.8                   # inside corner of the small back step
R_CONCAVE_J = 1.0                   # inside corner of the front wing step
R_FRONT_CORNER = 4.5                # corner between scoop and front flat
R_V = 12.0                          # fillet at the centre of the V

# --- screw posts & holes ------------------------------------------------------
BOSS_R = 2.4 * S
BOSS_HOLE_R = 1.6 * S               # insert bore from the top (blind)
BOSS_THRU_R = 0.9 * S               # small screw hole through the floor
BOSS_OFS_BACK = 3.1                 # post inset from the back edge (outer corner)
BOSS_OFS_SIDE = 2.7                 # post inset from the wing side edge
BOSS_OFS_FRONTC = 3.2               # post inset at the front-outer corner
BOSS_OFS_STEP = 2.9                 # post inset at the front step corner
BOSS_OFS_FRONT = (3.0, 2.6)         # post inset (from scoop, from front flat)
BOSS_SEG3_U = 48.0                  # post on the raised back section
BOSS_SEG3_OFS = 2.2                 # its inset from the back edge
FLOOR_HOLE_R = 0.9 * S
FLOOR_HOLES = [(-74.2, 21.2), (-28.9, -17.8)]      # left half (units)

# --- centre cable slot --------------------------------------------------------
SLOT_W = 10.0                       # width (units) of slot through back wall
SLOT_FLOOR = 0.5                    # slot stops this far above the floor

# ---------------------------------------------------------------------------
a = math.radians(WING_ANG)
U_DIR = (math.cos(a), -math.sin(a))     # along the wing back edge (left wing)
V_DIR = (math.sin(a), math.cos(a))      # outward (towards the back)


def rot(u, v):
    """wing-frame (u along back edge, v outward) -> world units (left wing)."""
    return (WING_ORG[0] + u * U_DIR[0] + v * V_DIR[0],
            WING_ORG[1] + u * U_DIR[1] + v * V_DIR[1])


def mir(p):
    return (-p[0], p[1])


def sc(p):
    return (p[0] * S, p[1] * S)


def heading(deg_below_x):
    h = math.radians(deg_below_x)
    return (math.cos(h), -math.sin(h))


# outline vertices of the left half (counter-clockwise, starting at the V)
p0 = rot(0, V_EDGE_V)
VC = rot(-p0[0] / U_DIR[0], V_EDGE_V)       # centre of the V (x = 0)
B = rot(STEP3_U, V_EDGE_V)
C = rot(STEP3_U, STEP2_V)
D = rot(STEP2_U, STEP2_V)
E = rot(STEP2_U, STEP1_V)
F = rot(STEP1_U, STEP1_V)
G = rot(STEP1_U, 0.0)
Hc = rot(0.0, 0.0)
I = rot(0.0, -WING_DEPTH)
J = rot(WING_FRONT_LEN, -WING_DEPTH)
K = rot(WING_FRONT_LEN, -WING_DEPTH - FRONT_STEP)
M = (-FRONT_HALF, FRONT_Y)

# scoop mid point: chord midpoint pushed into the part by SCOOP_SAG
chx, chy = M[0] - K[0], M[1] - K[1]
chl = math.hypot(chx, chy)
nx, ny = -chy / chl, chx / chl                 # left normal of chord (into part)
SM = ((K[0] + M[0]) / 2 + SCOOP_SAG * nx, (K[1] + M[1]) / 2 + SCOOP_SAG * ny)
T0 = heading(SCOOP_START_ANG)
T1 = heading(SCOOP_END_ANG)


def inset(p, d_in, d_out, c, c2=None):
    """point inset by c from the wall arriving at corner p and by c2 (default c)
    from the wall leaving it.  d_in / d_out: travel directions (CCW outline)."""
    c2 = c if c2 is None else c2
    n1 = (-d_in[1], d_in[0])
    n2 = (-d_out[1], d_out[0])
    # solve  (x - p).n1 = c ,  (x - p).n2 = c2
    det = n1[0] * n2[1] - n1[1] * n2[0]
    dx = (c * n2[1] - c2 * n1[1]) / det
    dy = (n1[0] * c2 - n2[0] * c) / det
    return (p[0] + dx, p[1] + dy)


mU = (-U_DIR[0], -U_DIR[1])
mV = (-V_DIR[0], -V_DIR[1])
_vl = math.hypot(VC[0] - B[0], VC[1] - B[1])
VDIR_OUT = ((B[0] - VC[0]) / _vl, (B[1] - VC[1]) / _vl)   # leaving centre (left)
VDIR_IN = (VDIR_OUT[0], -VDIR_OUT[1])                     # arriving (right half)
SM_T = (T0[0] + T1[0], T0[1] + T1[1])                     # scoop tangent at mid
SM_N = (-SM_T[1] / math.hypot(*SM_T), SM_T[0] / math.hypot(*SM_T))

# (corner, incoming dir, outgoing dir, radius, convex?) for the left half
corners = [
    (B, mU, V_DIR, R_CONCAVE_B, False),
    (C, V_DIR, mU, R_STEP_DOWN, True),
    (D, mU, mV, R_SMALL_STEP, True),
    (E, mV, mU, R_CONCAVE_E, False),
    (F, mU, mV, R_CONVEX, True),
    (G, mV, mU, R_CONCAVE, False),
    (Hc, mU, mV, R_BOSS_CORNER, True),
    (I, mV, U_DIR, R_BOSS_CORNER, True),
    (J, U_DIR, mV, R_CONCAVE_J, False),
    (K, mV, T0, R_STEP_CORNER, True),
    (M, T1, (1.0, 0.0), R_FRONT_CORNER, True),
]


def outline_prism(t, z0, h):
    """prism of the tray outline offset inwards by t units, from z0, height h,
    with its vertical corners rounded (radii adjusted for the offset)."""
    pts = [inset(VC, VDIR_IN, VDIR_OUT, t)] + [
        inset(p, din, dout, t) for (p, din, dout, r, cv) in corners]
    kk, mm = pts[-2], pts[-1]
    sm = (SM[0] + t * SM_N[0], SM[1] + t * SM_N[1])
    w = cq.Workplane("XY").workplane(offset=z0).moveTo(*sc(pts[0]))
    for p in pts[1:-1]:
        w = w.lineTo(*sc(p))
    w = w.spline([sc(sm), sc(mm)], tangents=[T0, T1], includeCurrent=True)
    w = w.lineTo(*sc(mir(mm)))
    w = w.spline([sc(mir(sm)), sc(mir(kk))],
                 tangents=[(T1[0], -T1[1]), (T0[0], -T0[1])], includeCurrent=True)
    for p in reversed(pts[1:-2]):
        w = w.lineTo(*sc(mir(p)))
    solid = w.close().extrude(h)

    jobs = [(pts[0], R_V + t)]
    for q, (p, din, dout, r, convex) in zip(pts[1:], corners):
        rr = r - t if convex else r + t
        jobs.append((q, rr))
        jobs.append((mir(q), rr))
    zc = z0 + h / 2
    for q, rr in jobs:
        if rr < 0.05:
            continue
        qs = sc(q)
        solid = solid.edges(
            cq.selectors.NearestToPointSelector((qs[0], qs[1], zc))).fillet(rr * S)
    return solid


# --- outer body and cavity ------------------------------------------------------------
outer = outline_prism(0.0, 0.0, H)
cavity = outline_prism(WALL / S, FLOOR, H)
body = outer.cut(cavity)


# --- screw posts ------------------------------------------------------------------
bosses_l = [
    inset(Hc, mU, mV, BOSS_OFS_BACK, BOSS_OFS_SIDE),  # back-outer corner
    inset(I, mV, U_DIR, BOSS_OFS_FRONTC),             # front-outer corner
    inset(K, mV, T0, BOSS_OFS_STEP),                  # front step corner
    inset(M, T1, (1.0, 0.0), *BOSS_OFS_FRONT),        # front flat corner
    rot(BOSS_SEG3_U, STEP2_V - BOSS_SEG3_OFS),        # raised back section
]
boss_pts = []
for p in bosses_l:
    boss_pts.append(sc(p))
    boss_pts.append(sc(mir(p)))

posts = (cq.Workplane("XY").workplane(offset=FLOOR / 2)
         .pushPoints(boss_pts).circle(BOSS_R).extrude(H - FLOOR / 2))
posts = posts.intersect(outer)
body = body.union(posts)

# --- centre cable slot through the back wall -------------------------------------------
slot = (cq.Workplane("XY").workplane(offset=FLOOR + SLOT_FLOOR * S)
        .center(0, sc(VC)[1])
        .rect(SLOT_W * S, 12 * S).extrude(H))
body = body.cut(slot)

# --- holes ------------------------------------------------------------------------------
bore = (cq.Workplane("XY").workplane(offset=FLOOR).pushPoints(boss_pts)
        .circle(BOSS_HOLE_R).extrude(H))
thru = (cq.Workplane("XY").workplane(offset=-1).pushPoints(boss_pts)
        .circle(BOSS_THRU_R).extrude(H + 2))
body = body.cut(bore).cut(thru)

fh = []
for p in FLOOR_HOLES:
    fh.append(sc(p))
    fh.append(sc(mir(p)))
holes = (cq.Workplane("XY").workplane(offset=-1).pushPoints(fh)
         .circle(FLOOR_HOLE_R).extrude(H))
body = body.cut(holes)

result = body
